import math
import cadquery as cq
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.BRep import BRep_Tool
from OCP.Geom import Geom_TrimmedCurve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.gp import gp_Ax2, gp_Circ, gp_Pnt, gp_Dir

# Wall-mount holder: rounded rectangular back plate (with 4 round pockets on
# its back), lofted flare into a round tube, tube continues as a grooved
# half-pipe rod.  A small snap barb on a slotted tongue sits under the tube.
# Plate back face lies on Y=0, the part extends towards -Y, tube axis on Z=0.

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 60.3        # plate width  (X)
PLATE_H = 21.8        # plate height (Z)
PLATE_T = 6.9         # plate thickness (Y)
PLATE_R = 4.0         # plate corner radius (in XZ)

FLARE_L = 7.8         # length of lofted transition plate -> tube

TUBE_R = 9.6          # big tube radius
TOTAL_L = 141.6       # plate back face to rod tip
STEP_Y = 91.3         # distance plate back -> end of the big tube
TUBE_SEAM = -142.5    # angular position of the tube surface seam (deg)

# rod (half-pipe) profile, same outer radius / axis as the big tube
ROD_CUT_Z = 1.65      # height of the flat underside of the rod above tube axis
ROD_FIL_OUT = 2.1     # rounding of the outer lobe corners
GROOVE_R = 4.3        # groove radius
GROOVE_TOP = 4.68     # height of the groove crown above tube axis
ROD_FIL_IN = 1.7      # rounding of the inner lobe corners

# pockets on the back face of the plate
POCKET_N = 4
POCKET_D = 9.5
POCKET_PITCH = 15.2
POCKET_DEPTH = 2.0

# snap barb underneath the big tube (Y positions measured from plate back)
BARB_Y0 = 63.2        # start of the ramp
BARB_Y1 = 70.3        # vertical catch face
BARB_H = 1.7          # radial height
BARB_W = 6.7          # width (X)
TONGUE_W = 6.9        # width of the tongue carrying the barb
NOTCH_Y1 = 75.2       # front end of the ramped notch ahead of the barb
NOTCH_D = 1.0         # notch depth at the barb catch face
SLOT_Y0 = 48.9        # rear end of the relief slots
SLOT_Y1 = 67.3        # front end of the relief slots (alongside the barb)
SLOT_W = 1.5          # relief slot width
SLOT_TOP = 2.4        # slot cut height above the tube bottom


# ---------------- helpers ----------------
def single_edge_wire(edges):
    """join tangent-continuous edges into one exact (rational) B-spline edge"""
    conv = GeomConvert_CompCurveToBSplineCurve()
    for e in edges:
        f, l = BRep_Tool.Range_s(e.wrapped)
        c = BRep_Tool.Curve_s(e.wrapped, f, l)
        conv.Add(Geom_TrimmedCurve(c, f, l), 1e-7, True)
    edge = cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge())
    return cq.Wire.assembleEdges([edge])


def rrect_wire(w, h, r, y):
    """rounded rectangle in the XZ plane at Y=y, one edge, seam at bottom"""
    a, b = w / 2, h / 2
    s = math.sqrt(0.5)

    def P(x, z):
        return cq.Vector(x, y, z)

    e = [
        cq.Edge.makeLine(P(0, -b), P(a - r, -b)),
        cq.Edge.makeThreePointArc(P(a - r, -b), P(a - r + r * s, -b + r - r * s), P(a, -b + r)),
        cq.Edge.makeLine(P(a, -b + r), P(a, b - r)),
        cq.Edge.makeThreePointArc(P(a, b - r), P(a - r + r * s, b - r + r * s), P(a - r, b)),
        cq.Edge.makeLine(P(a - r, b), P(-a + r, b)),
        cq.Edge.makeThreePointArc(P(-a + r, b), P(-a + r - r * s, b - r + r * s), P(-a, b - r)),
        cq.Edge.makeLine(P(-a, b - r), P(-a, -b + r)),
        cq.Edge.makeThreePointArc(P(-a, -b + r), P(-a + r - r * s, -b + r - r * s), P(-a + r, -b)),
        cq.Edge.makeLine(P(-a + r, -b), P(0, -b)),
    ]
    return single_edge_wire(e)


def circle_wire(r, y, seam_deg=180.0):
    """circle in the XZ plane at Y=y, same sense as rrect; seam_deg is the
    angle of the seam measured from +Z towards +X (180 = bottom)"""
    a = math.radians(seam_deg)
    ax = gp_Ax2(gp_Pnt(0, y, 0), gp_Dir(0, -1, 0),
                gp_Dir(math.sin(a), 0, math.cos(a)))
    e = cq.Edge(BRepBuilderAPI_MakeEdge(gp_Circ(ax, r)).Edge())
    return cq.Wire.assembleEdges([e])


def arc_mid(c, r, a, b):
    """midpoint of the short arc of circle (c, r) between points a and b"""
    ang_a = math.atan2(a[1] - c[1], a[0] - c[0])
    ang_b = math.atan2(b[1] - c[1], b[0] - c[0])
    d = ang_b - ang_a
    while d > math.pi:
        d -= 2 * math.pi
    while d < -math.pi:
        d += 2 * math.pi
    m = ang_a + d / 2
    return (c[0] + r * math.cos(m), c[1] + r * math.sin(m))


def mx(p):
    return (-p[0], p[1])


# ---------------- plate ----------------
plate_face = cq.Face.makeFromWires(rrect_wire(PLATE_W, PLATE_H, PLATE_R, 0.0))
plate = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(plate_face, cq.Vector(0, -PLATE_T, 0))
)

# ---------------- flare (loft rounded rectangle -> circle) ----------------
ts = BRepOffsetAPI_ThruSections(True, True, 1e-6)
ts.AddWire(rrect_wire(PLATE_W, PLATE_H, PLATE_R, -PLATE_T).wrapped)
ts.AddWire(circle_wire(TUBE_R, -PLATE_T - FLARE_L).wrapped)
ts.Build()
flare = cq.Workplane("XY").add(cq.Solid(ts.Shape()))

# ---------------- big tube ----------------
y_tube0 = PLATE_T + FLARE_L
tube_face = cq.Face.makeFromWires(circle_wire(TUBE_R, -y_tube0, TUBE_SEAM))
tube = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(tube_face, cq.Vector(0, -(STEP_Y - y_tube0), 0))
)

# ---------------- rod with grooved half-pipe profile ----------------
R = TUBE_R
zc = ROD_CUT_Z
ro = ROD_FIL_OUT
ri = ROD_FIL_IN
rg = GROOVE_R
zg = GROOVE_TOP - GROOVE_R

# outer lobe rounding: centre / tangent points
xo = math.sqrt((R - ro) ** 2 - (zc + ro) ** 2)
co = (xo, zc + ro)
k = R / (R - ro)
p_out = (co[0] * k, co[1] * k)          # tangent on tube circle
b_out = (xo, zc)                        # tangent on flat underside
# inner lobe rounding: centre / tangent points
xi = math.sqrt((rg + ri) ** 2 - (zc + ri - zg) ** 2)
ci = (xi, zc + ri)
b_in = (xi, zc)
kk = rg / (rg + ri)
p_in = (ci[0] * kk, zg + (ci[1] - zg) * kk)   # tangent on groove circle

rod_len = TOTAL_L - STEP_Y


rod = (
    cq.Workplane("XZ", origin=(0, -STEP_Y, 0))
    .moveTo(*p_out)
    .threePointArc((0, R), mx(p_out))
    .threePointArc(arc_mid(mx(co), ro, mx(p_out), mx(b_out)), mx(b_out))
    .lineTo(*mx(b_in))
    .threePointArc(arc_mid(mx(ci), ri, mx(b_in), mx(p_in)), mx(p_in))
    .threePointArc((0, GROOVE_TOP), p_in)
    .threePointArc(arc_mid(ci, ri, p_in, b_in), b_in)
    .lineTo(*b_out)
    .threePointArc(arc_mid(co, ro, b_out, p_out), p_out)
    .close()
    .extrude(rod_len)
)

body = plate.union(flare).union(tube).union(rod)

# ---------------- pockets in the back face ----------------
pockets = (
    cq.Workplane("XZ", origin=(0, POCKET_DEPTH, 0))
    .rarray(POCKET_PITCH, 1, POCKET_N, 1)
    .circle(POCKET_D / 2)
    .extrude(2 * POCKET_DEPTH)
)
body = body.cut(pockets)

# ---------------- snap barb under the tube ----------------
barb_len = BARB_Y1 - BARB_Y0
barb_prof = (
    cq.Workplane("YZ", origin=(-BARB_W / 2, 0, 0))
    .polyline([
        (-BARB_Y1, -R + 1.0),
        (-BARB_Y1, -R - BARB_H),
        (-BARB_Y0, -R + 0.3),
        (-BARB_Y0, -R + 1.0),
    ])
    .close()
    .extrude(BARB_W)
)
barb_env = (
    cq.Workplane("XZ", origin=(0, -BARB_Y0 + 1, 0))
    .circle(R + BARB_H)
    .extrude(barb_len + 2)
)
barb = barb_prof.intersect(barb_env)
body = body.union(barb)

# ---------------- relief slots behind the barb ----------------
slot_len = SLOT_Y1 - SLOT_Y0                      # length of the side slots
slot_xc = TONGUE_W / 2 + SLOT_W / 2               # side-slot centre lines
side_slots = (
    cq.Workplane("XY", origin=(0, 0, -R - 1.0))
    .pushPoints([(slot_xc, -(SLOT_Y0 + slot_len / 2)),
                 (-slot_xc, -(SLOT_Y0 + slot_len / 2))])
    .slot2D(slot_len, SLOT_W, angle=90)
    .extrude(1.0 + SLOT_TOP)
)
body = body.cut(side_slots)

# ---------------- ramped notch in front of the barb catch face ----------------
notch = (
    cq.Workplane("YZ", origin=(-BARB_W / 2, 0, 0))
    .polyline([
        (-BARB_Y1, -R + NOTCH_D),
        (-NOTCH_Y1, -R),
        (-NOTCH_Y1, -R - 3.0),
        (-BARB_Y1, -R - 3.0),
    ])
    .close()
    .extrude(BARB_W)
)
body = body.cut(notch)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
